import math
import cadquery as cq

# L-shaped corner block: top pockets with inclined floors, screw holes at the arm ends,
# recessed panels on the outer faces, wedge cavities on the inner faces, engraved label below.

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
W = 40.0            # outer size of the L footprint in X and in Y
T = 16.0            # arm thickness
H = 56.2            # height
R_IN = 1.2          # inner vertical corner fillet
EDGE_CH = 0.4       # small chamfer on the outer edges

END_CH_H = 4.4      # bottom chamfer at the arm ends, horizontal leg
END_CH_V = 7.9      # bottom chamfer at the arm ends, vertical leg

WALL_OUT = 2.2      # pocket wall to the outer faces
WALL_IN = 2.5       # pocket wall to the inner faces
RIB_W = 1.8         # diagonal rib width
RIB_X0 = 10.1       # rib centre line starts at (RIB_X0, 0) ...
RIB_X1 = 16.5       # ... and reaches (RIB_X1, T)
POCKET_D = 17.0     # depth of the pocket prisms (the floors below cut them shorter)
POCKET_OFF = 1.2    # inward draft offset of the pocket walls at full depth
POCKET_R = 1.35     # rounding of the pocket corners (plan, at the rim)
FLOOR_Z0 = 52.2     # pocket floor (front arm) is an inclined plane: height at the rib / inner wall corner
FLOOR_SY = 0.93     # ... rising this much per mm toward the inner wall
FLOOR_SX = 0.23     # ... and this much per mm toward the arm end
FLOOR_FIL = 1.5     # rounding of the valley between the floor and the outer wall
KITE_Z0 = 53.5      # corner pocket floor: narrow ledge along the outer walls at this height ...
KITE_BAND = 1.1     # ... reached by steeply drafted outer walls (plan inset of the ledge),
KITE_LEDGE = 1.6    # ... this wide,
KITE_SLOPE = 1.2    # ... from where it drops toward the inner corner (valley along the diagonal)
KITE_FIL = 1.0      # rounding of that valley
RIM_CH = 0.35       # chamfer on the pocket rims

HOLE_D = 5.0        # screw hole through the top
HOLE_END = 6.3      # hole centre distance from the arm end
HOLE_CH = 0.5       # chamfer at the top of the hole
HOLE_ARC_R = 5.1    # pocket end arc concentric with the hole
BORE_D = 7.5        # head bore above the side cavity
BORE_TOP = 48.6     # top of that bore
LOW_HOLE_D = 6.6    # hole from the underside up into the cavity

PANEL_INSET = 3.2   # recessed panel on the outer faces
PANEL_DEPTH = 0.9
PANEL_BEVEL = 1.4
PANEL_R = 1.2       # corner rounding of the panel floor outline

IN_PANEL_DEPTH = 0.5   # shallow recess on the inner faces
IN_PANEL_END = 2.1     # border at the arm end and at the bottom
IN_PANEL_R = 1.5       # corner rounding of the inner recess

CAV_TOP = 54.6      # wedge cavity on the inner faces: top edge at the face
CAV_BOT = 36.9      # flat floor of the cavity
CAV_SLOPE = 0.67    # dX/dZ of the cavity ceiling
CAV_END = 37.5      # cavity runs along the arm up to here
CAV_R = 1.8         # rounding at the far end of the cavity

DIMPLE_D = 4.5      # small blind hole in the underside
DIMPLE_DEPTH = 2.0

LABEL = "V1.02"     # version label engraved in the underside of the back arm
LABEL_SIZE = 6.0
LABEL_DEPTH = 0.4
LABEL_X = 4.2       # label centre line (distance from the outer face X = 0)
LABEL_Y = 22.6      # label centre along the back arm

hole_c = W - HOLE_END   # hole centre coordinate along the arm

# ---------------- base L block ----------------
l_pts = [(0, 0), (W, 0), (W, T), (T, T), (T, W), (0, W)]
body = cq.Workplane("XY").polyline(l_pts).close().extrude(H)
body = body.edges("|Z").edges(cq.selectors.NearestToPointSelector((T, T, H / 2))).fillet(R_IN)
body = body.faces(">Z or <Z").edges().chamfer(EDGE_CH)


def outer_vertical(e):
    bb = e.BoundingBox()
    return bb.zlen > H * 0.5 and not (abs(bb.xmin - T) < 2 and abs(bb.ymin - T) < 2)


body = body.newObject([e for e in body.edges().vals() if outer_vertical(e)]).chamfer(EDGE_CH)

# bottom chamfers at the two arm ends (triangular prisms)
ch_prof = [(W - END_CH_H - END_CH_H / END_CH_V, -1.0), (W + 2, -1.0), (W + 2, END_CH_V + 2 * END_CH_V / END_CH_H), (W, END_CH_V)]
ch_front = cq.Workplane("XZ").polyline(ch_prof).close().extrude(-(T + 2)).translate((0, -1, 0))
ch_back = cq.Workplane("YZ").polyline(ch_prof).close().extrude(T + 2).translate((-1, 0, 0))
body = body.cut(ch_front).cut(ch_back)

# ---------------- recessed panels on the two outer faces ----------------
outline_pts = [(0, 0), (W - END_CH_H, 0), (W, END_CH_V), (W, H), (0, H)]


def panel_tool():
    # profile drawn in the XZ plane, floor at depth PANEL_DEPTH, bevelled walls opening to the face
    wire = (
        cq.Workplane("XZ").polyline(outline_pts).close()
        .offset2D(-(PANEL_INSET + PANEL_BEVEL + PANEL_R), "intersection")
        .offset2D(PANEL_R, "arc")
    )
    ang = math.degrees(math.atan2(PANEL_BEVEL, PANEL_DEPTH))
    floor = wire.extrude(PANEL_DEPTH + 1.0, taper=-ang)  # XZ normal is -Y: grows toward -Y
    return floor.translate((0, PANEL_DEPTH, 0))


front_panel = panel_tool()
body = body.cut(front_panel)
left_panel = front_panel.mirror(mirrorPlane=cq.Vector(1, -1, 0))
body = body.cut(left_panel)


# ---------------- shallow recess on the two inner faces ----------------
def inner_panel_tool():
    # for the back arm inner face (plane X = T), profile in (Y, Z), offset inward from the face outline
    top = CAV_TOP + IN_PANEL_END
    yz = [(T - 6.0, 0), (W - END_CH_H, 0), (W, END_CH_V), (W, top), (T - 6.0, top)]
    return (
        cq.Workplane("YZ", origin=(T - IN_PANEL_DEPTH, 0, 0))
        .polyline(yz).close()
        .offset2D(-(IN_PANEL_END + IN_PANEL_R), "intersection")
        .offset2D(IN_PANEL_R, "arc")
        .extrude(IN_PANEL_DEPTH + 1.0)
    )


in_back = inner_panel_tool()
in_front = in_back.mirror(mirrorPlane=cq.Vector(1, -1, 0))
body = body.cut(in_back).cut(in_front)

# ---------------- wedge cavities on the inner faces ----------------
def cavity_tool():
    x_bot = T - CAV_SLOPE * (CAV_TOP - CAV_BOT)
    xz = [
        (x_bot, CAV_BOT),
        (T + 2.0, CAV_BOT),
        (T + 2.0, CAV_TOP + 2.0 / CAV_SLOPE),
    ]
    tool = (
        cq.Workplane("XZ", origin=(0, CAV_END, 0))
        .polyline(xz).close().extrude(CAV_END - T + IN_PANEL_DEPTH)
    )
    # round the far end of the cavity (edges lying in the plane Y = CAV_END)
    tool = tool.edges(cq.selectors.BoxSelector((x_bot - 1, CAV_END - 0.01, CAV_BOT - 1), (T + 0.01, CAV_END + 0.01, CAV_TOP + 1)))
    tool = tool.edges("not |X").fillet(CAV_R)
    return tool


cav_back = cavity_tool()
cav_front = cav_back.mirror(mirrorPlane=cq.Vector(1, -1, 0))
body = body.cut(cav_back).cut(cav_front)

# ---------------- top pockets ----------------
k = (RIB_X1 - RIB_X0) / T                  # rib slope dX/dY
half = (RIB_W / 2) * math.sqrt(1 + k * k)  # horizontal half width of the rib


def rib_x(y, side):
    return RIB_X0 + k * y + side * half


def _n(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def corner_fillet(prev, v, nxt, r):
    """tangent points and arc mid point of a fillet of radius r at corner v"""
    ui = _n((v[0] - prev[0], v[1] - prev[1]))
    uo = _n((nxt[0] - v[0], nxt[1] - v[1]))
    cos_t = -(ui[0] * uo[0] + ui[1] * uo[1])
    th = math.acos(max(-1.0, min(1.0, cos_t)))
    t = r / math.tan(th / 2)
    p_in = (v[0] - ui[0] * t, v[1] - ui[1] * t)
    p_out = (v[0] + uo[0] * t, v[1] + uo[1] * t)
    b = _n((-ui[0] + uo[0], -ui[1] + uo[1]))
    m = r / math.sin(th / 2) - r
    mid = (v[0] + b[0] * m, v[1] + b[1] * m)
    return p_in, mid, p_out


def rounded_polygon_edges(pts, r):
    n = len(pts)
    fil = [corner_fillet(pts[i - 1], pts[i], pts[(i + 1) % n], r) for i in range(n)]
    edges = []
    for i in range(n):
        p_in, mid, p_out = fil[i]
        edges.append(cq.Edge.makeThreePointArc(cq.Vector(*p_in, 0), cq.Vector(*mid, 0), cq.Vector(*p_out, 0)))
        nxt_in = fil[(i + 1) % n][0]
        edges.append(cq.Edge.makeLine(cq.Vector(*p_out, 0), cq.Vector(*nxt_in, 0)))
    return edges


def arc_edge(c, rad, a0, a1):
    am = 0.5 * (a0 + a1)
    p = lambda a: cq.Vector(c[0] + rad * math.cos(a), c[1] + rad * math.sin(a), 0)
    return cq.Edge.makeThreePointArc(p(a0), p(am), p(a1))


def arm_pocket_edges():
    """pocket of the front arm: rib side, two long sides, concave arc around the hole, all corners rounded"""
    y0, y1 = WALL_OUT, T - WALL_IN
    hc, yc = hole_c, T / 2
    rr = POCKET_R
    big = HOLE_ARC_R
    a = (rib_x(y0, 1), y0)
    d = (rib_x(y1, 1), y1)
    c1 = (hc - math.sqrt((big + rr) ** 2 - (yc - y0 - rr) ** 2), y0 + rr)
    c2 = (hc - math.sqrt((big + rr) ** 2 - (y1 - rr - yc) ** 2), y1 - rr)
    t1 = (c1[0], y0)
    t2 = (c2[0], y1)
    ang1 = math.atan2(c1[1] - yc, c1[0] - hc)
    ang2 = math.atan2(c2[1] - yc, c2[0] - hc)
    p1 = (hc + big * math.cos(ang1), yc + big * math.sin(ang1))
    p2 = (hc + big * math.cos(ang2), yc + big * math.sin(ang2))
    fa_in, fa_mid, fa_out = corner_fillet(d, a, t1, rr)
    fd_in, fd_mid, fd_out = corner_fillet(t2, d, a, rr)
    V = lambda p: cq.Vector(p[0], p[1], 0)
    e = []
    e.append(cq.Edge.makeThreePointArc(V(fa_in), V(fa_mid), V(fa_out)))
    e.append(cq.Edge.makeLine(V(fa_out), V(t1)))
    # convex fillet t1 -> p1 (centre c1), goes from angle -90 deg to the direction of the hole centre
    a_start = -math.pi / 2
    a_end = math.atan2(p1[1] - c1[1], p1[0] - c1[0])
    e.append(arc_edge(c1, rr, a_start, a_end))
    # concave arc p1 -> p2 around the hole (through the point facing -X)
    e.append(cq.Edge.makeThreePointArc(V(p1), V((hc - big, yc)), V(p2)))
    a_start = math.atan2(p2[1] - c2[1], p2[0] - c2[0])
    e.append(arc_edge(c2, rr, a_start, math.pi / 2))
    e.append(cq.Edge.makeLine(V(t2), V(fd_in)))
    e.append(cq.Edge.makeThreePointArc(V(fd_in), V(fd_mid), V(fd_out)))
    e.append(cq.Edge.makeLine(V(fd_out), V(fa_in)))
    return e


apex = (RIB_X0 - half) / (1 - k)
corner_pts = [
    (WALL_OUT, WALL_OUT),
    (rib_x(WALL_OUT, -1), WALL_OUT),
    (apex, apex),
    (WALL_OUT, rib_x(WALL_OUT, -1)),
]


def pocket_tool(edges):
    wire = cq.Wire.assembleEdges(edges).translate(cq.Vector(0, 0, H))
    ang = math.degrees(math.atan2(POCKET_OFF, POCKET_D))
    face = cq.Face.makeFromWires(wire)
    solid = cq.Solid.extrudeLinear(face, cq.Vector(0, 0, -POCKET_D), taper=ang)
    return cq.Workplane("XY").add(solid)


def half_space_above(point, normal):
    """big block whose bottom face is the plane through point with the (upward) normal"""
    n = cq.Vector(*normal).normalized()
    blk = cq.Workplane("XY").box(300, 300, 150, centered=(True, True, False))
    z_axis = cq.Vector(0, 0, 1)
    axis = z_axis.cross(n)
    if axis.Length > 1e-9:
        blk = blk.rotate((0, 0, 0), axis.toTuple(), math.degrees(math.acos(z_axis.dot(n))))
    return blk.translate(point)


def above_floor_front():
    # half space above the inclined floor plane of the front arm pocket
    return half_space_above((RIB_X1, T - WALL_IN, FLOOR_Z0), (-FLOOR_SX, -FLOOR_SY, 1.0))


def above_floor_corner():
    # corner pocket: steep band down the outer walls to a narrow ledge, then two planes falling
    # toward the inner corner (valley along the diagonal)
    x_e = WALL_OUT + KITE_BAND + KITE_LEDGE
    ledge = half_space_above((0, 0, KITE_Z0), (0, 0, 1))
    fall_x = half_space_above((x_e, 0, KITE_Z0), (KITE_SLOPE, 0, 1))
    fall_y = half_space_above((0, x_e, KITE_Z0), (0, KITE_SLOPE, 1))
    tan_b = KITE_BAND / (H - KITE_Z0)
    band_x = half_space_above((WALL_OUT, 0, H + 0.3), (1.0, 0, tan_b))
    band_y = half_space_above((0, WALL_OUT, H + 0.3), (0, 1.0, tan_b))
    return ledge.union(fall_x.intersect(fall_y)).intersect(band_x).intersect(band_y)


def round_filler(p0, n1, n2, r, length=60.0):
    """material that rounds the concave valley between two planes (unit normals n1, n2 pointing into
    the pocket) meeting along the line through p0; subtracted from a pocket tool"""
    e = n1.cross(n2).normalized()
    a = r / (1 + n1.dot(n2))
    c = p0 + n1 * a + n2 * a
    t1 = c - n1 * r
    t2 = c - n2 * r
    u = (n1 - e * n1.dot(e)).normalized()
    v = e.cross(u)
    loc = lambda q: ((q - p0).dot(u), (q - p0).dot(v))
    plane = cq.Plane(origin=(p0 - e * (length / 2)).toTuple(), xDir=u.toTuple(), normal=e.toTuple())
    quad = cq.Workplane(plane).polyline([(0, 0), loc(t1), loc(c), loc(t2)]).close().extrude(length)
    disk = cq.Workplane(plane).center(*loc(c)).circle(r).extrude(length)
    return quad.cut(disk)


def valley_filler():
    """rounds the valley between the inclined floor and the drafted outer wall of the front arm pocket"""
    kt = POCKET_OFF / POCKET_D
    n1 = cq.Vector(0, 1, kt).normalized()                       # outer wall, facing into the pocket
    n2 = cq.Vector(-FLOOR_SX, -FLOOR_SY, 1.0).normalized()      # floor, facing up
    xr = RIB_X1                                                 # a point on the valley line at X = RIB_X1
    y = (WALL_OUT + (H - FLOOR_Z0 + FLOOR_SY * (T - WALL_IN)) * kt) / (1 + FLOOR_SY * kt)
    z = FLOOR_Z0 + FLOOR_SY * (y - (T - WALL_IN))
    return round_filler(cq.Vector(xr, y, z), n1, n2, FLOOR_FIL)


def kite_valley_filler():
    """rounds the valley of the corner pocket floor along the diagonal"""
    x_e = WALL_OUT + KITE_BAND + KITE_LEDGE
    n1 = cq.Vector(KITE_SLOPE, 0, 1).normalized()
    n2 = cq.Vector(0, KITE_SLOPE, 1).normalized()
    q = 10.0
    p0 = cq.Vector(q, q, KITE_Z0 - KITE_SLOPE * (q - x_e))
    return round_filler(p0, n1, n2, KITE_FIL, 40.0)


space_front = above_floor_front()
fill_front = valley_filler()
p_corner = (
    pocket_tool(rounded_polygon_edges(corner_pts, POCKET_R))
    .intersect(above_floor_corner())
    .cut(kite_valley_filler())
)
p_front = pocket_tool(arm_pocket_edges()).intersect(space_front).cut(fill_front)
p_back = p_front.mirror(mirrorPlane=cq.Vector(1, -1, 0))
for p in (p_corner, p_front, p_back):
    body = body.cut(p)


def dist_to_outline(p):
    best = 1e9
    n = len(l_pts)
    for i in range(n):
        ax, ay = l_pts[i]
        bx, by = l_pts[(i + 1) % n]
        dx, dy = bx - ax, by - ay
        t = max(0.0, min(1.0, ((p.x - ax) * dx + (p.y - ay) * dy) / (dx * dx + dy * dy)))
        best = min(best, math.hypot(p.x - (ax + t * dx), p.y - (ay + t * dy)))
    return best


top_face = body.faces(">Z")
def on_kite_band(p):
    # rim of the corner pocket along the outer walls: already bevelled by the steep band
    return p.x < T and p.y < T and min(p.x, p.y) < WALL_OUT + 1.0


rim_edges = [
    e for e in top_face.edges().vals()
    if dist_to_outline(e.Center()) > 1.5 and abs(e.Center().z - H) < 1e-3 and not on_kite_band(e.Center())
]
body = body.newObject(rim_edges).chamfer(RIM_CH)

# ---------------- holes ----------------
for (hx, hy) in ((hole_c, T / 2), (T / 2, hole_c)):
    top_hole = cq.Workplane("XY").center(hx, hy).circle(HOLE_D / 2).extrude(H + 1)
    csk = (
        cq.Workplane("XY", origin=(0, 0, H - HOLE_CH))
        .center(hx, hy).circle(HOLE_D / 2).extrude(HOLE_CH + 1, taper=-45)
    )
    bore = cq.Workplane("XY", origin=(0, 0, CAV_BOT - 1)).center(hx, hy).circle(BORE_D / 2).extrude(BORE_TOP - CAV_BOT + 1)
    low = cq.Workplane("XY", origin=(0, 0, -1)).center(hx, hy).circle(LOW_HOLE_D / 2).extrude(CAV_BOT + 1.5)
    body = body.cut(top_hole).cut(csk).cut(bore).cut(low)

# small blind hole in the underside of the corner
dimple = cq.Workplane("XY", origin=(0, 0, -1)).center(T / 2, T / 2).circle(DIMPLE_D / 2).extrude(DIMPLE_DEPTH + 1)
body = body.cut(dimple)

# engraved label, readable from below (reads toward the corner)
try:
    label_plane = cq.Plane(origin=(LABEL_X, LABEL_Y, 0), xDir=(0, -1, 0), normal=(0, 0, -1))
    label = cq.Workplane(label_plane).text(
        LABEL, LABEL_SIZE, -LABEL_DEPTH, combine=False, halign="center", valign="center"
    )
    engraved = body.cut(label)
    if engraved.val().isValid():
        body = engraved
except Exception:
    pass

result = body
